import cadquery as cq
import math

# =====================================================================
#  "flomon FM-101A" snap-on cover: shallow open cup with a quadrilateral
#  rounded outline, chamfered top plateau carrying a raised logo, a clip
#  slot in the front skirt and raised lettering on the inside.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
# plan outline: quadrilateral (sharp corners) before rounding
P_BL = (-48.7, -20.8)   # front-left  (-X,-Y)
P_BR = (48.7, -20.8)    # front-right (+X,-Y)
P_TR = (43.7, 23.2)     # back-right  (+X,+Y)
P_TL = (-44.4, 18.0)    # back-left   (-X,+Y)
QUAD = [P_BL, P_BR, P_TR, P_TL]
R_CORNER = 9.0          # plan corner radius
H_WALL = 9.4            # height of the vertical outer wall
CH_TOP = 1.7            # 45 deg chamfer up to the top plateau
H = H_WALL + CH_TOP     # overall height (without logo)
T_WALL = 1.8            # skirt wall thickness
T_TOP = 2.0             # top plate thickness
ZC = H - T_TOP          # ceiling height of the underside cavity
CH_IN = 1.7             # chamfer where inner walls meet the ceiling
R_IN = [6.5, 7.2, 7.2, 8.5]     # cavity corner radii (BL, BR, TR, TL)
T_LEFT = 2.6            # thicker left (-X) end skirt

# clip slot in the front skirt
SLOT_X = 26.5
SLOT_W = 10.2
SLOT_H = 1.8
SLOT_R = 0.6

T_PAD = 2.4             # local skirt thickness behind the slot
PAD_EXT = 0.8           # pad overhang beyond each slot end

# shallow clip recesses in the inner skirt faces (no inner chamfer there)
REC_D = 0.8             # recess depth into the skirt
REC_FRONT = (8.8, 20.6)     # x-range on the front (-Y) wall
REC_BACK = (19.7, 33.3)     # x-range on the back (+Y) wall
REC_LEFT = (0.6, 7.6)       # y-range on the left (-X) end wall

# raised logo on the top plateau
LOGO_H = 0.4            # emboss height
W_ARC = 1.9             # stroke width of the wave arcs
W_DROP = 2.0            # stroke width of the drop ring
W_TXT = 2.2             # stroke width of the letters
DROP_C = (-19.15, -0.36)    # centre of the drop (and of the wave arcs)
DROP_RO, DROP_TIP_O = 5.6, 9.3          # outer drop: radius, centre->tip
DROP_CI = (-19.2, 0.0)
DROP_RI, DROP_TIP_I = 3.6, 5.8          # inner drop
DROP_TILT = -6.0        # tilt of the outer drop tip (deg, + = ccw)
DROP_TILT_I = -2.0       # tilt of the inner drop tip
ARC_R = [8.93, 12.94, 17.1]     # centre-line radii of the three waves
ARC_HALF = [36.0, 37.0, 38.0]   # half opening angle of each wave (deg)
ARC_MID = 184.0                 # direction of the wave mid-points (deg)
BASE_Y = -5.0           # letter centre-line baseline
XH_Y = 2.3              # letter centre-line x-height
ASC_Y = 5.8             # letter centre-line ascender height

# raised "FM-101A" on the cavity ceiling (reads from below, +Y = up)
TXT_H = 0.4
TXT_W = 1.8
TXT_B, TXT_T = -6.8, 4.1    # centre-line bottom / top (world Y)


def rounded_quad(r, inset=0.0, z0=0.0):
    """Quadrilateral outline with corner radius r, shrunk by `inset`."""
    w = (cq.Workplane("XY").workplane(offset=z0).polyline(QUAD).close()
         .offset2D(-r, "intersection"))
    return w.offset2D(r - inset, "arc")


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY").box(x1 - x0, y1 - y0, z1 - z0)
            .translate(((x0 + x1) / 2, (y0 + y1) / 2, (z0 + z1) / 2)))


# ---------------- main body ----------------
body = rounded_quad(R_CORNER).extrude(H)
body = body.faces(">Z").edges().chamfer(CH_TOP)

# hollow underside (open cup); every skirt side has its own thickness
def inset_quad(ins):
    """Sharp quadrilateral with edge i (QUAD[i] -> QUAD[i+1]) moved inwards by ins[i]."""
    lines = []
    for i in range(4):
        (x0, y0), (x1, y1) = QUAD[i], QUAD[(i + 1) % 4]
        dx, dy = x1 - x0, y1 - y0
        ln = math.hypot(dx, dy)
        nx, ny = -dy / ln, dx / ln
        lines.append(((x0 + nx * ins[i], y0 + ny * ins[i]), (dx / ln, dy / ln)))
    pts = []
    for j in range(4):
        (p, d), (q, e) = lines[j - 1], lines[j]
        den = d[0] * e[1] - d[1] * e[0]
        t = ((q[0] - p[0]) * e[1] - (q[1] - p[1]) * e[0]) / den
        pts.append((p[0] + d[0] * t, p[1] + d[1] * t))
    return pts      # corner j sits at QUAD[j]


def cavity(ins, radii, z1):
    pts = inset_quad(ins)
    f = cq.Face.makeFromWires(cq.Wire.makePolygon([cq.Vector(x, y, 0) for x, y in pts], close=True))
    for (cx, cy), r in zip(pts, radii):
        vt = [v for v in f.Vertices() if abs(v.X - cx) < 1e-6 and abs(v.Y - cy) < 1e-6]
        f = f.fillet2D(r, vt)
    return cq.Workplane("XY").add(cq.Solid.extrudeLinear(f, cq.Vector(0, 0, z1)))


T_SIDES = [T_WALL, T_WALL, T_WALL, T_LEFT]     # front, right, back, left
pocket = cavity(T_SIDES, R_IN, ZC)
pocket = pocket.faces(">Z").edges().chamfer(CH_IN)
body = body.cut(pocket)

# clip recesses: locally thinner skirt, no inner chamfer
for ins, reg in (([T_WALL - REC_D] * 4, box(REC_FRONT[0], REC_FRONT[1], -30, -10, -1, ZC + 1)),
                 ([T_WALL - REC_D] * 4, box(REC_BACK[0], REC_BACK[1], 10, 30, -1, ZC + 1)),
                 ([T_WALL] * 4, box(-60, -35, REC_LEFT[0], REC_LEFT[1], -1, ZC + 1))):
    wide = cavity(ins, R_IN, ZC)
    body = body.cut(wide.intersect(reg))

# thickened pad behind the slot
pad_y0 = P_BL[1] + 0.5
body = body.union(box(SLOT_X - SLOT_W / 2 - PAD_EXT, SLOT_X + SLOT_W / 2 + PAD_EXT,
                      pad_y0, P_BL[1] + T_PAD, 0, ZC - 0.3))

# slot through the front wall at the rim
slot = (cq.Workplane("XZ").workplane(offset=15)
        .center(SLOT_X, 0)
        .sketch().rect(SLOT_W, 2 * SLOT_H).vertices().fillet(SLOT_R).finalize()
        .extrude(10))
body = body.cut(slot)


# ---------------- helpers for raised strokes ----------------
def wp(z):
    return cq.Workplane("XY").workplane(offset=z)


def stroke(path_fn, w, z, h):
    """Thicken an open centre-line path into a round-capped raised stroke."""
    return path_fn(wp(z)).offset2D(w / 2.0, "arc").extrude(h)


def straight(p0, p1, w, z, h):
    """Straight round-capped stroke between two centre-line points."""
    dx, dy = p1[0] - p0[0], p1[1] - p0[1]
    ln = math.hypot(dx, dy)
    return (wp(z).center((p0[0] + p1[0]) / 2.0, (p0[1] + p1[1]) / 2.0)
            .slot2D(ln + w, w, math.degrees(math.atan2(dy, dx))).extrude(h))


def pol(c, r, a):
    return (c[0] + r * math.cos(math.radians(a)), c[1] + r * math.sin(math.radians(a)))


def drop_face(c, r, tip_d, tilt, z, tip_r):
    """Tear-drop: circle plus two tangents to a (slightly rounded) tip."""
    ang = 90.0 + tilt
    tip = pol(c, tip_d, ang)
    beta = math.degrees(math.acos(r / tip_d))
    t1 = pol(c, r, ang - beta)
    t2 = pol(c, r, ang + beta)
    bot = pol(c, r, ang + 180.0)
    wire = (cq.Workplane("XY").workplane(offset=z).moveTo(*tip).lineTo(*t2)
            .threePointArc(bot, t1).close()).wires().val()
    f = cq.Face.makeFromWires(wire)
    vt = [v for v in f.Vertices()
          if abs(v.X - tip[0]) < 1e-6 and abs(v.Y - tip[1]) < 1e-6]
    return f.fillet2D(tip_r, vt)


# ---------------- raised logo on the top ----------------
ZT = H - 0.01
HT = LOGO_H + 0.01
logo = []
# three wave arcs around the drop
for r, h in zip(ARC_R, ARC_HALF):
    a0, a1 = ARC_MID - h, ARC_MID + h
    p0, pm, p1 = pol(DROP_C, r, a0), pol(DROP_C, r, ARC_MID), pol(DROP_C, r, a1)
    logo.append(stroke(lambda w, p0=p0, pm=pm, p1=p1: w.moveTo(*p0).threePointArc(pm, p1),
                       W_ARC, ZT, HT))

# drop ring
d_out = cq.Solid.extrudeLinear(drop_face(DROP_C, DROP_RO, DROP_TIP_O, DROP_TILT, ZT, 0.9),
                               cq.Vector(0, 0, HT))
d_in = cq.Solid.extrudeLinear(drop_face(DROP_CI, DROP_RI, DROP_TIP_I, DROP_TILT_I, ZT - 0.5, 0.5),
                              cq.Vector(0, 0, HT + 1.0))
logo.append(cq.Workplane("XY").add(d_out.cut(d_in)))

# letters "flomon"
FX = -9.4               # stem of the f
HK = 2.4                # radius of the hook of the f
F_TOP = 6.0             # centre-line top of the hook
logo.append(stroke(lambda w: w.moveTo(FX, BASE_Y).lineTo(FX, F_TOP - HK)
                   .threePointArc((FX + HK - HK * math.cos(math.radians(45)),
                                   F_TOP - HK + HK * math.sin(math.radians(45))),
                                  (FX + HK, F_TOP)), W_TXT, ZT, HT))
logo.append(straight((-10.9, 2.05), (-6.6, 2.05), W_TXT, ZT, HT))
logo.append(straight((-2.95, BASE_Y), (-2.95, ASC_Y), W_TXT, ZT, HT))


def o_ring(cx, cy, rx, ry, w, z, h):
    o = wp(z).center(cx, cy).ellipse(rx + w / 2, ry + w / 2).extrude(h)
    i = wp(z - 0.5).center(cx, cy).ellipse(rx - w / 2, ry - w / 2).extrude(h + 1.0)
    return o.cut(i)


def arch(x0, x1, y_end0, y_end1, ytop):
    """Stem up at x0, semicircular arch over to x1, stem down at x1."""
    r = (x1 - x0) / 2.0
    yc = ytop - r
    return lambda w: (w.moveTo(x0, y_end0).lineTo(x0, yc)
                      .threePointArc((x0 + r, ytop), (x1, yc)).lineTo(x1, y_end1))


logo.append(o_ring(4.1, -1.35, 3.0, 3.6, W_TXT, ZT, HT))                     # o
logo.append(stroke(arch(10.4, 15.25, BASE_Y, -1.9, XH_Y), W_TXT, ZT, HT))    # m
logo.append(stroke(arch(15.25, 20.1, -1.9, BASE_Y, XH_Y), W_TXT, ZT, HT))
logo.append(o_ring(26.15, -1.35, 3.0, 3.6, W_TXT, ZT, HT))                   # o
logo.append(stroke(arch(32.9, 38.7, BASE_Y, BASE_Y, XH_Y), W_TXT, ZT, HT))   # n

for f in logo:
    body = body.union(f)

# ---------------- raised "FM-101A" on the cavity ceiling ----------------
ZI = ZC - TXT_H          # strokes hang down from the ceiling
HI = TXT_H + 0.01
hh = TXT_T - TXT_B
txt = []


def seg(p0, p1):
    txt.append(straight(p0, p1, TXT_W, ZI, HI))


# F  (letter "left" is +X because the text reads from below)
xf = 33.8
seg((xf, TXT_B), (xf, TXT_T))
seg((xf, TXT_T), (xf - 6.0, TXT_T))
seg((xf, TXT_B + 0.55 * hh), (xf - 4.8, TXT_B + 0.55 * hh))
# M
x0m, x1m = 24.5, 15.1
seg((x0m, TXT_B), (x0m, TXT_T))
seg((x1m, TXT_B), (x1m, TXT_T))
seg((x0m, TXT_T), ((x0m + x1m) / 2, TXT_B + 0.3 * hh))
seg(((x0m + x1m) / 2, TXT_B + 0.3 * hh), (x1m, TXT_T))
# -
seg((10.5, -2.64), (6.9, -2.64))
# 1
for x1 in (0.2, -18.0):
    seg((x1, TXT_B), (x1, TXT_T))
    seg((x1, TXT_T), (x1 + 2.4, TXT_T - 2.4))
# slashed zero
xo = -7.6
yo = (TXT_B + TXT_T) / 2
txt.append(o_ring(xo, yo, 3.0, hh / 2, TXT_W, ZI, HI))
seg((xo + 2.2, TXT_B + 1.5), (xo - 2.2, TXT_T - 1.5))
# A
seg((-30.1, TXT_B), (-26.3, TXT_T))
seg((-26.3, TXT_T), (-22.6, TXT_B))
seg((-29.0, TXT_B + 0.3 * hh), (-23.6, TXT_B + 0.3 * hh))

for f in txt:
    body = body.union(f)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
